import math
import cadquery as cq

# ------------------------------------------------------------------
# Ride-on toy tractor / go-kart : seat on an L-post, rear battery box,
# flat chassis with foot plate, small motor with pulley, 4 wheels.
# All driving dimensions below are in "design units"; U converts to mm.
# X = driving direction (front at +X), Y = left/right, Z = up.
# ------------------------------------------------------------------
U = 2.0  # mm per design unit

# wheels
REAR_D, REAR_W = 68.0, 10.7
REAR_X, REAR_Z = 0.0, 34.3
FRONT_D, FRONT_W = 62.0, 10.3
FRONT_X, FRONT_Z = 173.0, 29.3
WHEEL_Y_OUT = 59.0           # outer face of all wheels
HUB_HOLE_D = 4.5

# rear box
BOX_X0, BOX_X1 = -18.5, 18.5
BOX_Z0, BOX_Z1 = 30.0, 74.5
BOX_Y = 48.3

# chassis
BASE_X0, BASE_X1 = 62.0, 139.2
BASE_Z0, BASE_Z1 = 32.6, 38.7
PLATE_HALF_W = 27.6
RAIL_IN = 21.4
GROOVE_W, GROOVE_D = 3.0, 3.6
FOOT_X0, FOOT_X1 = 71.3, 139.2
FOOT_Z1 = 44.9
FOOT_HOLE_X, FOOT_HOLE_D = 126.4, 16.0
FAXLE_W = 6.7
FAXLE_Z0, FAXLE_Z1 = 25.9, 32.6

CROSS_X0, CROSS_X1 = 61.6, 86.7
CROSS_Z0, CROSS_Z1 = 26.4, 32.6
CROSS_HALF = 49.5
TRAY_IN = 27.5
TRAY_RIM = 2.4
TRAY_DEPTH = 2.6

RAIL_A_X0, RAIL_A_X1 = 18.5, 72.0
RAIL_A_Z0, RAIL_A_Z1 = 37.7, 43.9
RAIL_A_HALF = 4.25

# motor (axis in the horizontal plane, yawed towards -Y at the front)
MOTOR_D, MOTOR_L = 12.6, 26.0
MOTOR_FRONT = (67.3, -22.0)
MOTOR_Z = 47.1
MOTOR_YAW = 28.0
PULLEY_X, PULLEY_Y, PULLEY_D, PULLEY_T = 73.3, -25.8, 13.0, 2.9
PULLEY_Z0 = 45.5
BELT_PIN = (78.4, -1.0)
BELT_PIN_D = 4.4
PIN_TOP = 51.0

# seat post / arm / bracket
POST_X0, POST_X1 = 32.4, 50.8
POST_HALF = 12.2
ARM_X1 = 116.6
ARM_Z0, ARM_Z1 = 70.9, 78.2
BRK_X0, BRK_X1 = 92.0, 117.7
BRK_WALL = 3.4
BRK_Z0, BRK_ZP = 51.2, 54.9
BRK_PLATE_HALF = 15.5

# seat cushion
CUSH_X0, CUSH_X1 = 7.7, 70.0
CUSH_Z0 = 102.9
CUSH_HALF_REAR, CUSH_HALF_FRONT = 39.5, 44.4
CUSH_DIP = 6.5           # depth of the centre channel between bolsters
CUSH_CH_HALF = 22.0      # half width of channel floor

# backrest
BACK_TOP = 171.4
BACK_PANEL_HALF = 16.0


def P(x, z):
    return (x * U, z * U)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box((x1 - x0) * U, (y1 - y0) * U, (z1 - z0) * U)
            .translate(((x0 + x1) / 2 * U, (y0 + y1) / 2 * U, (z0 + z1) / 2 * U)))


def ycyl(d, y0, y1, x, z):
    return (cq.Workplane("XZ", origin=(0, y0 * U, 0))
            .center(x * U, z * U).circle(d / 2 * U).extrude(-(y1 - y0) * U))


def zcyl(d, x, y, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0 * U))
            .center(x * U, y * U).circle(d / 2 * U).extrude((z1 - z0) * U))


def wheel(d, w, x, z, side):
    y_out = side * WHEEL_Y_OUT
    y_in = side * (WHEEL_Y_OUT - w)
    y0, y1 = min(y_out, y_in), max(y_out, y_in)
    wh = ycyl(d, y0, y1, x, z)
    hole = ycyl(HUB_HOLE_D, y0 - 1, y1 + 1, x, z)
    return wh.cut(hole)


def xz_profile(pts_fn, half):
    """extrude a closed XZ profile symmetrically in Y (single face, no seam)"""
    wp = pts_fn(cq.Workplane("XZ", origin=(0, half * U, 0)))
    return wp.close().extrude(2 * half * U)


parts = []

# ---------------- wheels ----------------
for s in (-1, 1):
    parts.append(wheel(REAR_D, REAR_W, REAR_X, REAR_Z, s))
    parts.append(wheel(FRONT_D, FRONT_W, FRONT_X, FRONT_Z, s))

# rear axle (hidden in box) and front axle beam
parts.append(ycyl(4.0, -WHEEL_Y_OUT + REAR_W, WHEEL_Y_OUT - REAR_W, REAR_X, REAR_Z))
parts.append(box(FRONT_X - FAXLE_W / 2, FRONT_X + FAXLE_W / 2,
                 -(WHEEL_Y_OUT - FRONT_W), WHEEL_Y_OUT - FRONT_W, FAXLE_Z0, FAXLE_Z1))

# ---------------- rear box ----------------
parts.append(box(BOX_X0, BOX_X1, -BOX_Y, BOX_Y, BOX_Z0, BOX_Z1))

# ---------------- chassis ----------------
base = box(BASE_X0, BASE_X1, -PLATE_HALF_W, PLATE_HALF_W, BASE_Z0, BASE_Z1)
rail_end = FRONT_X + FAXLE_W / 2
for s in (-1, 1):
    # C-channel side rails, web outboard, opening facing the centre line
    y0, y1 = sorted((s * RAIL_IN, s * PLATE_HALF_W))
    rail = box(BASE_X1 - 1, rail_end, y0, y1, BASE_Z0, BASE_Z1)
    g0, g1 = sorted((s * (RAIL_IN - 1.0), s * (RAIL_IN + GROOVE_D)))
    rail = rail.cut(box(BASE_X1 + 1.5, rail_end + 1, g0, g1,
                        BASE_Z0 + GROOVE_W / 2, BASE_Z1 - GROOVE_W / 2))
    base = base.union(rail)
# plate is a ladder frame seen from below: shallow pocket in its underside
base = base.cut(box(CROSS_X1 + 0.5, BASE_X1 - 3.0, -RAIL_IN, RAIL_IN,
                    BASE_Z0 - 1, BASE_Z0 + 3.0))
foot = box(FOOT_X0, FOOT_X1, -PLATE_HALF_W, PLATE_HALF_W, BASE_Z1, FOOT_Z1)
plates = base.union(foot)
plates = plates.cut(zcyl(FOOT_HOLE_D, FOOT_HOLE_X, 0, 20, 60))
# shallow pocket under the seat bracket with a through window and small slots
plates = plates.cut(box(85.0, 112.0, -18.6, 18.6, FOOT_Z1 - 3.5, 60))
plates = plates.cut(box(86.0, 106.0, -8.0, 17.0, 20, 60))
plates = plates.cut(box(106.0, 110.0, 3.0, 12.0, FOOT_Z1 - 4.0, 60))
# small hooked tab standing in the pocket
tab = box(93.0, 94.6, -16.5, -12.5, FOOT_Z1 - 3.6, FOOT_Z1 - 0.3)
tab = tab.union(box(93.0, 96.5, -16.5, -15.0, FOOT_Z1 - 1.6, FOOT_Z1 - 0.3))
plates = plates.union(tab)
parts.append(plates)

# cross member with an open tray (pocket + slot) at each end
cross = box(CROSS_X0, CROSS_X1, -CROSS_HALF, CROSS_HALF, CROSS_Z0, CROSS_Z1)
cross = cross.edges("|Z").edges("<X").fillet(4.0 * U)
for s in (-1, 1):
    yi, yo = sorted((s * (TRAY_IN + TRAY_RIM), s * (CROSS_HALF - TRAY_RIM)))
    pocket = box(CROSS_X0 + TRAY_RIM, CROSS_X1 - TRAY_RIM, yi, yo,
                 CROSS_Z1 - TRAY_DEPTH, CROSS_Z1 + 1)
    pocket = pocket.edges("|Z").edges("<X").fillet(2.0 * U)
    cross = cross.cut(pocket)
    ys0, ys1 = sorted((s * (CROSS_HALF - TRAY_RIM - 2.6), s * (CROSS_HALF - TRAY_RIM - 8.2)))
    cross = cross.cut(box(72.0, 83.5, ys0, ys1, CROSS_Z0 - 1, CROSS_Z1))
parts.append(cross)

# central longitudinal rail from rear box to foot plate
parts.append(box(RAIL_A_X0, RAIL_A_X1, -RAIL_A_HALF, RAIL_A_HALF, RAIL_A_Z0, RAIL_A_Z1))
parts.append(zcyl(2.2, 34.8, 0.0, RAIL_A_Z1, 50.0))

# ---------------- motor, pulley, belt ----------------
yaw = math.radians(MOTOR_YAW)
motor = (cq.Workplane("YZ")
         .circle(MOTOR_D / 2 * U).extrude(-MOTOR_L * U)
         .edges().fillet(1.0 * U)
         .rotate((0, 0, 0), (0, 0, 1), -MOTOR_YAW)
         .translate((MOTOR_FRONT[0] * U, MOTOR_FRONT[1] * U, MOTOR_Z * U)))
ring = (cq.Workplane("YZ").circle(MOTOR_D / 2 * U + 0.4 * U).extrude(-2.0 * U)
        .rotate((0, 0, 0), (0, 0, 1), -MOTOR_YAW)
        .translate(((MOTOR_FRONT[0] - 3.0 * math.cos(yaw)) * U,
                    (MOTOR_FRONT[1] + 3.0 * math.sin(yaw)) * U, MOTOR_Z * U)))
parts.append(motor.union(ring))

pulley = zcyl(PULLEY_D, PULLEY_X, PULLEY_Y, PULLEY_Z0, PULLEY_Z0 + PULLEY_T)
pulley = pulley.union(zcyl(1.6, PULLEY_X, PULLEY_Y, PULLEY_Z0, PIN_TOP + 0.5))
pin = zcyl(BELT_PIN_D, BELT_PIN[0], BELT_PIN[1], FOOT_Z1, PIN_TOP)
# flat belt: hull of pulley rim and pin
dx, dy = BELT_PIN[0] - PULLEY_X, BELT_PIN[1] - PULLEY_Y
L = math.hypot(dx, dy)
ux, uy = dx / L, dy / L
nx, ny = -uy, ux
r1, r2 = PULLEY_D / 2, BELT_PIN_D / 2
belt_pts = [(PULLEY_X + nx * r1, PULLEY_Y + ny * r1),
            (BELT_PIN[0] + nx * r2, BELT_PIN[1] + ny * r2),
            (BELT_PIN[0] - nx * r2, BELT_PIN[1] - ny * r2),
            (PULLEY_X - nx * r1, PULLEY_Y - ny * r1)]
belt = (cq.Workplane("XY", origin=(0, 0, (PULLEY_Z0 + 0.9) * U))
        .polyline([(x * U, y * U) for x, y in belt_pts]).close().extrude(1.2 * U))
parts.append(pulley.union(pin).union(belt))

# ---------------- seat post, arm, bracket ----------------
post = box(POST_X0, POST_X1, -POST_HALF, POST_HALF, ARM_Z0, CUSH_Z0 + 1)
arm = box(POST_X0, ARM_X1, -POST_HALF, POST_HALF, ARM_Z0, ARM_Z1)
brk = box(BRK_X0 + 1, BRK_X0 + 1 + BRK_WALL, -POST_HALF, POST_HALF, BRK_ZP, ARM_Z0 + 0.5)
brk = brk.union(box(ARM_X1 - BRK_WALL, ARM_X1, -POST_HALF, POST_HALF, BRK_ZP, ARM_Z0 + 0.5))
bplate = box(BRK_X0, BRK_X1, -BRK_PLATE_HALF, BRK_PLATE_HALF, BRK_Z0, BRK_ZP)
bplate = bplate.edges("|Y").fillet(1.2 * U)
brk = brk.union(bplate)
parts.append(post.union(arm).union(brk))

# ---------------- seat cushion ----------------
top_curve = [(34.2, 119.5), (52.7, 123.0), (64.2, 121.0), (CUSH_X1, 116.0)]


def cush_side(wp):
    return (wp.moveTo(*P(CUSH_X0, CUSH_Z0))
            .lineTo(*P(CUSH_X1, CUSH_Z0))
            .lineTo(*P(CUSH_X1, top_curve[-1][1]))
            .spline([P(x, z) for x, z in reversed(top_curve[:-1])] + [P(CUSH_X0, 115.6)],
                    includeCurrent=True))


cush = xz_profile(cush_side, CUSH_HALF_FRONT + 1)
# plan-view outline: narrower at the back, rounded front corners
plan = (cq.Workplane("XY", origin=(0, 0, (CUSH_Z0 - 2) * U))
        .moveTo(CUSH_X0 * U, -CUSH_HALF_REAR * U)
        .spline([P(36.0, -43.0), P(58.0, -CUSH_HALF_FRONT)], includeCurrent=True)
        .lineTo(CUSH_X1 * U, -CUSH_HALF_FRONT * U)
        .lineTo(CUSH_X1 * U, CUSH_HALF_FRONT * U)
        .lineTo(58.0 * U, CUSH_HALF_FRONT * U)
        .spline([P(36.0, 43.0), P(CUSH_X0, CUSH_HALF_REAR)], includeCurrent=True)
        .close()
        .extrude(30 * U))
plan = plan.edges("|Z").edges(">X").fillet(5.0 * U)
plan = plan.edges("|Z").edges("<X").fillet(6.0 * U)
cush = cush.intersect(plan)
try:
    cush = cush.faces("<Z").edges().fillet(3.5 * U)
except Exception:
    pass

# centre channel between the side bolsters: a ramp-shaped profile swept along
# the seat's top curve lowered by CUSH_DIP (flat floor, bolsters rising outwards)
floor_pts = [(-6.0, 107.6), (CUSH_X0, 115.6 - CUSH_DIP)] + \
    [(x, z - CUSH_DIP) for x, z in top_curve[:-1]] + [(CUSH_X1, 110.5), (78.0, 106.0)]
path = cq.Workplane("XZ").spline([P(x, z) for x, z in floor_pts],
                                 tangents=[(1.0, 0.08), (1.0, -0.5)])
ramp = [(CUSH_CH_HALF, 0.0), (29.0, 1.4), (37.0, 3.8), (CUSH_HALF_FRONT, 6.6),
        (56.0, 13.0)]
x_s, z_s = floor_pts[0]
chan = (cq.Workplane("YZ", origin=(x_s * U, 0, z_s * U))
        .moveTo(-ramp[-1][0] * U, ramp[-1][1] * U)
        .spline([(-y * U, z * U) for y, z in reversed(ramp[:-1])], includeCurrent=True,
                tangents=[(1.0, -0.55), (1.0, 0.0)])
        .lineTo(ramp[0][0] * U, 0.0)
        .spline([(y * U, z * U) for y, z in ramp[1:]], includeCurrent=True,
                tangents=[(1.0, 0.0), (1.0, 0.55)])
        .lineTo(ramp[-1][0] * U, 30.0 * U)
        .lineTo(-ramp[-1][0] * U, 30.0 * U)
        .close()
        .sweep(path, transition="right"))
cush = cush.cut(chan)
parts.append(cush)

# ---------------- backrest ----------------


def back_side(wp):
    return (wp.moveTo(*P(-3.9, 114.6))
            .lineTo(*P(5.4, 114.4))
            .spline([P(8.6, 116.8), P(10.0, 124.8), P(9.5, 131.7), P(5.4, 150.2),
                     P(0.1, BACK_TOP)], includeCurrent=True)
            .lineTo(*P(-25.3, BACK_TOP))
            .spline([P(-24.6, 161.7), P(-22.3, 150.2), P(-17.7, 138.7), P(-11.9, 127.1),
                     P(-3.9, 114.6)], includeCurrent=True))


back = xz_profile(back_side, 42.0)
# front-view outline: barrel shaped, widest at mid height
front_outline = (cq.Workplane("YZ", origin=(-40 * U, 0, 0))
                 .moveTo(*P(-28.0, 108.0))
                 .spline([P(-34.0, 118.0), P(-38.2, 126.6), P(-40.6, 140.0),
                          P(-39.8, 157.7), P(-36.0, BACK_TOP + 0.8)], includeCurrent=True)
                 .lineTo(*P(36.0, BACK_TOP + 0.8))
                 .spline([P(39.8, 157.7), P(40.6, 140.0), P(38.2, 126.6), P(34.0, 118.0),
                          P(28.0, 108.0)], includeCurrent=True)
                 .close()
                 .extrude(80 * U))
back = back.intersect(front_outline)
# recessed centre panel between the side wings
tilt = math.degrees(math.atan2(15.0, 55.4))
# plan section of the recess: flat panel, then an S-shaped flank easing out
# onto the wing fronts (local x = depth towards the front, local y = Y)
flank_s = [(0.0, BACK_PANEL_HALF), (1.6, BACK_PANEL_HALF + 4.0), (5.5, BACK_PANEL_HALF + 8.5),
           (10.0, BACK_PANEL_HALF + 13.0), (13.0, BACK_PANEL_HALF + 17.5),
           (14.0, BACK_PANEL_HALF + 22.0)]
recess = (cq.Workplane("XY")
          .moveTo(0.0, -BACK_PANEL_HALF * U)
          .lineTo(0.0, BACK_PANEL_HALF * U)
          .spline([(x * U, y * U) for x, y in flank_s[1:]], includeCurrent=True,
                  tangents=[(0.0, 1.0), (0.0, 1.0)])
          .lineTo(40 * U, flank_s[-1][1] * U)
          .lineTo(40 * U, -flank_s[-1][1] * U)
          .lineTo(flank_s[-1][0] * U, -flank_s[-1][1] * U)
          .spline([(x * U, -y * U) for x, y in reversed(flank_s[:-1])], includeCurrent=True,
                  tangents=[(0.0, 1.0), (0.0, 1.0)])
          .close()
          .extrude(90 * U)
          .translate((0, 0, -20 * U))
          .rotate((0, 0, 0), (0, 1, 0), -tilt)
          .translate((6.0 * U, 0, 116.0 * U)))
back = back.cut(recess)
try:
    back = back.faces(">Z").edges().fillet(2.5 * U)
except Exception:
    pass
parts.append(back)

result = parts[0]
for p in parts[1:]:
    result = result.union(p)

VIEW = {"azimuth": 45, "elevation": 26}
